import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 196.0        # overall length along Y (measured on the outer +X side)
W = 30.0         # overall width along X
H = 30.0         # overall height along Z
T = 9.0          # thickness of the upright wall (at +X)
B = 9.0          # thickness of the base plate
FLAT = 4.6       # width of the flat on top of the wall (rest is the bevel)
E_CAP = 5.0      # thickness of the closed end cap at -Y
R_END = 5.8      # vertical fillets on the outer corners of the closed end
R_IN = 2.5       # fillet between end cap and wall inside the channel
R_FLOOR = 1.0    # fillet along the floor of the channel (inner corners)
R_MITER = 3.2    # fillet on the obtuse (-X) corner of the miter
CUT_Z = 5.5      # corner cut at the sharp bottom tip of the miter: height on the tip edge
CUT_Y = 7.8      #   length along the outer bottom edge
CUT_M = 6.5      #   length along the mitred bottom edge
C_BOT = 0.7      # small chamfer around the bottom face

# blind hole in the outer face of the wall
WH_Y = 33.9      # distance from the closed end
WH_Z = 15.9      # height of hole centre
WH_D = 7.0
WH_DEPTH = 6.0
WH_CH = 0.4

# countersunk hole through the base plate
BH_X = 14.7      # from the -X edge
BH_Y = 94.3      # from the closed end
BH_D = 5.8
BH_CSK = 10.4

VIEW = {"azimuth": 45, "elevation": 26}

# slope of the bevel plane that forms the end-cap top and the wall bevel
SLOPE = (H - B) / (W - FLAT)


def z_bevel(x):
    return B + x * SLOPE


# ---------------- plan outline, extruded to full height ----------------
# miter: 45 deg line from (0, L - W) to (W, L); obtuse corner at (0, L - W) rounded
t_m = R_MITER * math.tan(math.radians(22.5))        # tangent length at the 135 deg corner
m_a = (0.0, L - W - t_m)                            # tangent point on the -X side
m_b = (t_m / math.sqrt(2), L - W + t_m / math.sqrt(2))  # tangent point on the miter
# point on the arc (bisector direction)
c_m = (R_MITER, L - W - t_m)                        # arc centre
ang_mid = math.radians(180 - 22.5)
m_mid = (c_m[0] + R_MITER * math.cos(ang_mid), c_m[1] + R_MITER * math.sin(ang_mid))

plan = (
    cq.Workplane("XY")
    .moveTo(R_END, 0)
    .lineTo(W - R_END, 0)
    .radiusArc((W, R_END), -R_END)
    .lineTo(W, L)
    .lineTo(*m_b)
    .threePointArc(m_mid, m_a)
    .lineTo(0, R_END)
    .radiusArc((R_END, 0), -R_END)
    .close()
    .extrude(H)
)
body = plan

# channel pocket above the base plate, inside the wall, beyond the end cap
pocket = (
    cq.Workplane("XY").workplane(offset=B)
    .moveTo(-5, E_CAP)
    .lineTo(W - T - R_IN, E_CAP)
    .radiusArc((W - T, E_CAP + R_IN), R_IN)
    .lineTo(W - T, L + 20)
    .lineTo(-5, L + 20)
    .close()
    .extrude(H)
)
body = body.cut(pocket)

# round the concave edges where the channel floor meets the wall and the end cap
body = body.edges(cq.selectors.BoxSelector((1.0, E_CAP - 0.1, B - 0.1),
                                           (W - T + 0.1, L - 40, B + 0.1))).fillet(R_FLOOR)

# single bevel plane: slanted top of the end cap and bevel on the wall top
bevel = (
    cq.Workplane("XZ")
    .polyline([(-5, z_bevel(-5)), (W + 5, z_bevel(W + 5)),
               (W + 5, H + 40), (-5, H + 40)]).close()
    .extrude(-(L + 20)).translate((0, -10, 0))
)
body = body.cut(bevel)

# corner cut at the acute bottom tip of the miter
p1 = cq.Vector(W, L, CUT_Z)
p2 = cq.Vector(W, L - CUT_Y, 0)
p3 = cq.Vector(W - CUT_M / math.sqrt(2), L - CUT_M / math.sqrt(2), 0)
n = (p2 - p1).cross(p3 - p1).normalized()
tip = cq.Vector(W, L, 0)
if n.dot(tip - p1) < 0:
    n = -n
plane = cq.Plane(origin=p1, xDir=(p2 - p1).normalized(), normal=n)
corner_cut = cq.Workplane(plane).rect(60, 60).extrude(30)
body = body.cut(corner_cut)

# small chamfer around the bottom face
body = body.faces("<Z").edges().chamfer(C_BOT)

# ---------------- holes ----------------
# blind hole in the outer wall face with a small entry chamfer
wall_hole = cq.Solid.makeCylinder(WH_D / 2, WH_DEPTH + 1,
                                  pnt=cq.Vector(W + 1, WH_Y, WH_Z), dir=cq.Vector(-1, 0, 0))
wall_ch = cq.Solid.makeCone(WH_D / 2 + WH_CH + 1, WH_D / 2, WH_CH + 1,
                            pnt=cq.Vector(W + 1, WH_Y, WH_Z), dir=cq.Vector(-1, 0, 0))
body = body.cut(cq.Workplane().add(wall_hole)).cut(cq.Workplane().add(wall_ch))

# countersunk through hole in the base plate
csk_depth = (BH_CSK - BH_D) / 2.0
base_hole = cq.Solid.makeCylinder(BH_D / 2, B + 2, pnt=cq.Vector(BH_X, BH_Y, -1),
                                  dir=cq.Vector(0, 0, 1))
csk = cq.Solid.makeCone(BH_D / 2, BH_CSK / 2 + 1, csk_depth + 1,
                        pnt=cq.Vector(BH_X, BH_Y, B - csk_depth), dir=cq.Vector(0, 0, 1))
body = body.cut(cq.Workplane().add(base_hole)).cut(cq.Workplane().add(csk))

result = body
